import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
SHAFT_D = 10.0          # shank diameter = thread major diameter
HEAD_D = 20.0           # countersunk cone top diameter (flush with bar top)
CONE_DEPTH = 5.0        # axial depth of the cone (90 deg countersink)
BAR_W = 6.5             # bar width (X)
BAR_L = 32.8            # bar length (Y)
BAR_H = 7.4             # bar height (Z)
TOTAL_H = 35.0          # overall height, bar bottom to shaft tip
THREAD_L = 7.55         # threaded length at the tip
PITCH = 2.03            # thread pitch (right hand, single start)
THREAD_DEPTH = 1.05     # radial thread depth
CREST_W = 0.1           # flat width left at the thread crest
FLANK_ANGLE = 40.0      # flank angle from the radial direction (80 deg V)
CREST_PHASE = 0.5       # distance below the tip of the first crest on the +X side
HELIX_START = 90.0      # angle where the helix segments start (hidden side)

R = SHAFT_D / 2.0
RH = HEAD_D / 2.0
R_CORE = R - THREAD_DEPTH
z_cone_bot = BAR_H - CONE_DEPTH
z_ts = TOTAL_H - THREAD_L          # start of the threaded section

# ---------------- revolved body: foot, countersunk cone, shank ----------------
# profile drawn in the YZ plane so the revolve seam lies along +Y (inside the bar)
body_pts = [
    (0, 0),
    (R, 0),
    (R, z_cone_bot),
    (RH, BAR_H),
    (R, BAR_H),
    (R, TOTAL_H),
    (0, TOTAL_H),
]
body = (
    cq.Workplane("YZ")
    .polyline(body_pts)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)

# ---------------- bar (T-head) ----------------
bar = cq.Workplane("XY").box(BAR_W, BAR_L, BAR_H, centered=(True, True, False))

blank = bar.union(body)


# ---------------- helical thread groove ----------------
def make_groove():
    """Helical V groove with a rounded root, swept along a right-hand helix
    on the root diameter and limited to the threaded length."""
    tan_f = math.tan(math.radians(FLANK_ANGLE))
    root_w = PITCH - CREST_W - 2.0 * THREAD_DEPTH * tan_f      # flat at the root
    r_out = R + 0.5                                            # cutter reaches outside
    r_fl = R + 0.01                                            # flanks end just outside
    w_top = root_w + 2.0 * (r_fl - R_CORE) * tan_f
    # groove centre half a pitch below the crest on +X
    z_g = TOTAL_H - CREST_PHASE - PITCH / 2.0 + PITCH * HELIX_START / 360.0
    n_back = math.ceil((z_g - (z_ts - PITCH)) / PITCH)
    z_h0 = z_g - n_back * PITCH
    n_turns = math.ceil(((TOTAL_H + PITCH) - z_h0) / PITCH)
    # helix path built from one-turn segments starting on +Y (keeps the swept
    # faces small so the booleans stay robust)
    seg = cq.Wire.makeHelix(pitch=PITCH, height=PITCH, radius=R_CORE).Edges()[0]
    edges = [
        seg.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), HELIX_START).translate(
            cq.Vector(0, 0, PITCH * k))
        for k in range(n_turns)
    ]
    path = cq.Wire.assembleEdges(edges)
    # groove profile in (radius, z): straight flanks blended by a root arc
    # that is tangent to both flanks and to the root (minor) diameter
    a = root_w / 2.0
    rho = a / (math.sqrt(1.0 + tan_f ** 2) - tan_f)              # root radius
    s = (rho - a * tan_f) / math.sqrt(1.0 + tan_f ** 2)
    r_t = R_CORE + s / math.sqrt(1.0 + tan_f ** 2)               # tangent point
    z_t = a + s * tan_f / math.sqrt(1.0 + tan_f ** 2)
    ca, sa = math.cos(math.radians(HELIX_START)), math.sin(math.radians(HELIX_START))

    def P(r, z):
        return cq.Vector(r * ca, r * sa, z)

    wire = cq.Wire.assembleEdges([
        cq.Edge.makeLine(P(r_out, -w_top / 2), P(r_fl, -w_top / 2)),
        cq.Edge.makeLine(P(r_fl, -w_top / 2), P(r_t, -z_t)),
        cq.Edge.makeThreePointArc(P(r_t, -z_t), P(R_CORE, 0.0), P(r_t, z_t)),
        cq.Edge.makeLine(P(r_t, z_t), P(r_fl, w_top / 2)),
        cq.Edge.makeLine(P(r_fl, w_top / 2), P(r_out, w_top / 2)),
        cq.Edge.makeLine(P(r_out, w_top / 2), P(r_out, -w_top / 2)),
    ])
    groove = cq.Solid.sweep(wire, [], path, makeSolid=True, isFrenet=True)
    groove = groove.translate(cq.Vector(0, 0, z_h0))
    # the groove runs out flat at the start of the threaded length
    slab = cq.Solid.makeCylinder(R + 1.0, THREAD_L + 1.0, cq.Vector(0, 0, z_ts))
    return groove.intersect(slab)


v_blank = blank.val().Volume()
result = None
try:
    groove = make_groove()
    cut = blank.cut(cq.Workplane("XY").add(groove))
    v_cut = cut.val().Volume()
    removed = v_blank - v_cut
    # groove volume inside the shank is roughly 1/4..1/2 of the threaded ring volume
    ring = math.pi * (R ** 2 - R_CORE ** 2) * THREAD_L
    if len(cut.solids().vals()) == 1 and 0.2 * ring < removed < 0.7 * ring and cut.val().isValid():
        result = cut
except Exception:
    result = None

if result is None:
    # fallback: annular V grooves (plain geometry)
    tan_f = math.tan(math.radians(FLANK_ANGLE))
    half_top = (PITCH - CREST_W) / 2.0
    half_root = half_top - THREAD_DEPTH * tan_f
    cutters = None
    n = int(THREAD_L / PITCH)
    for k in range(n):
        zc = TOTAL_H - CREST_PHASE - PITCH / 2.0 - k * PITCH
        g = (
            cq.Workplane("YZ")
            .polyline([(R_CORE, zc - half_root), (R + 0.5, zc - half_top - 0.5 * tan_f),
                       (R + 0.5, zc + half_top + 0.5 * tan_f), (R_CORE, zc + half_root)])
            .close()
            .revolve(360, (0, 0, 0), (0, 1, 0))
        )
        cutters = g if cutters is None else cutters.union(g)
    result = blank.cut(cutters)

VIEW = {"azimuth": 45, "elevation": 26}
